import math
import cadquery as cq

# ---------------------------------------------------------------
# Units: model built in "grid units" then scaled by K to millimetres
# Axes: X across (width), Y front(0)->back(+), Z top(0)->down(-)
# ---------------------------------------------------------------
K = 0.5            # mm per grid unit

HW = 61.5          # half width of top plate
L = 190.5          # top plate length (front edge Y=0 -> back edge)
T = 9.0            # top plate thickness
TAB_HW = 33.85     # half width of rear tab
TAB_D = 14.8       # rear tab depth

WIN_HW = 20.4      # top window half width (also rear shaft)
WIN_Y0, WIN_Y1 = 115.8, 186.4
NOTCH_HW, NOTCH_Y1 = 9.0, 192.8

FW_Y = 9.3         # front wall face position
FW_T = 12.0        # front wall thickness

ALPHA = 27.0       # tilt of the front clamp block (deg)
P1 = (52.9, -28.2) # top-back corner of tilted block (Y, Z)
BL = 89.0          # tilted block length (along tilt)
BH = 76.5          # tilted block height
LIP = 14.9         # lip (tongue) thickness on top of block
LIP_R = 6.0        # lip front rounding
SLOT_HW = 18.3     # centre slot half width
CORE_HW = 24.6     # core (between legs) half width
JAW_U0 = 74.7      # back of jaws (along tilt)
BR_U0, BR_H = 84.0, 7.5   # front bridge across centre slot
JAW_V0, JAW_V1 = 28.8, 59.8
FOOTJ_V0 = 68.5
GROOVE_U0, GROOVE_V0, GROOVE_V1 = 77.4, 8.5, 24.0
JAW_HOLE_X = 42.9
JAW_HOLE_U = 82.0

BACK_Y = 114.0     # rear edge of side legs
WALL_BOT = -100.0  # bottom of side legs
STRIP_BOT = -28.2  # bottom of rear upper strip
STRIP_T = 5.0      # rear strip thickness

BOX_Y1 = 173.8     # rear foot slot start
BP_Y0 = 181.1      # back band front face
FOOT_TOP, FOOT_BOT = -103.1, -117.6
FOOT_Y0 = 143.5
TUBE_IN_HW, TUBE_Z0, TUBE_Z1 = 15.4, -96.6, -63.5
TUBE_TOP = -57.5
TUBE_Y1 = 177.6
TUBE_Y0 = 70.0


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def mirror_x(wp):
    return wp.union(wp.mirror("YZ"))


ca = math.cos(math.radians(ALPHA))
sa = math.sin(math.radians(ALPHA))


def tilt_pt(u, v):
    """local (u along tilt forward, v along tilt downward) -> (Y, Z)"""
    return (P1[0] - ca * u + sa * v, P1[1] - sa * u - ca * v)


def lbox(x0, x1, u0, u1, v0, v1):
    """box in the (unrotated) local tilted frame: u -> -Y, v -> -Z"""
    return box(x0, x1, -u1, -u0, -v1, -v0)


def place(wp):
    return wp.rotate((0, 0, 0), (1, 0, 0), ALPHA).translate((0, P1[0], P1[1]))


def yz_prism(pts, x0, x1):
    return (cq.Workplane("YZ").polyline(pts).close().extrude(x1 - x0)
            .translate((x0, 0, 0)))


# ---------------- top plate ----------------
plate = box(-HW, HW, 0, L, -T, 0).union(box(-TAB_HW, TAB_HW, L - 1, L + TAB_D, -T, 0))
holes_small = [(0, 196.0), (0, 107.2)]
holes_big = [(-40.9, 57.4), (43.1, 52.0), (0, 15.4)]
for (x, y) in holes_small:
    plate = plate.cut(cq.Workplane("XY").center(x, y).circle(2.75).extrude(30).translate((0, 0, -15)))
for (x, y) in holes_big:
    plate = plate.cut(cq.Workplane("XY").center(x, y).circle(4.3).extrude(30).translate((0, 0, -15)))

# ---------------- side blocks (walls + legs) ----------------
a_top = tilt_pt(41.3, -LIP)       # where lip top meets front wall
a_line = tilt_pt(41.3, 0)
leg_a = tilt_pt(0, 59.5)
leg_d = tilt_pt(-1.1, 67.5)
leg_e = tilt_pt(-1.1, 75.2)
prof = [
    (FW_Y, -T), (L, -T), (L, STRIP_BOT), (BP_Y0, STRIP_BOT), (BP_Y0, -14.3),
    (BOX_Y1, -14.3), (BOX_Y1, STRIP_BOT), (BACK_Y, STRIP_BOT), (BACK_Y, WALL_BOT),
    (98.4, -90.5), leg_e, leg_d, leg_a, P1, a_line, a_top,
]
side = yz_prism(prof, WIN_HW, HW)
# strap slot in the front face of the leg (outer part only)
side = side.cut(place(lbox(CORE_HW, HW + 1, -15.0, 5.0, 59.5, 67.5)))
# rear part of the side is only a thin strip hanging from the plate
side = side.cut(box(WIN_HW - 1, HW - STRIP_T, BACK_Y + 0.01, BP_Y0, STRIP_BOT - 1, -T - 0.01))
# bolt hole through the floor of the strap slot in the leg
side = side.cut(place(cq.Workplane("XY").center(JAW_HOLE_X, 4.5).circle(2.4)
                      .extrude(45).translate((0, 0, -67.5 - 25))))
for yh in (71.9, 107.4):
    side = side.cut(cq.Workplane("YZ").center(yh, -49.3).circle(2.9).extrude(35)
                    .translate((HW - 30, 0, 0)))
# rear band (back end of strip) with a bolt hole
band = box(WIN_HW, HW, BP_Y0, L, STRIP_BOT, -T)
band = band.cut(cq.Workplane("XZ").center(42.0, -22.5).circle(2.75).extrude(-40).translate((0, 170, 0)))
side = side.cut(box(WIN_HW, HW + 1, BP_Y0, L + 1, STRIP_BOT - 1, -T - 0.01)).union(band)

# rear box walls (continuation of the core) and feet
bwall = box(WIN_HW, CORE_HW, BACK_Y - 1, L, WALL_BOT - 0.5, -T)
bwall = bwall.union(box(WIN_HW, CORE_HW, FOOT_Y0, L, FOOT_TOP, -T))
foot = box(WIN_HW, HW, FOOT_Y0, L, FOOT_BOT, FOOT_TOP)
foot = foot.cut(box(28.0, HW + 1, BOX_Y1, BP_Y0, FOOT_BOT - 1, FOOT_TOP + 1))
foot = foot.cut(cq.Workplane("XZ").center(43.5, -110.35).circle(2.75).extrude(-12).translate((0, BP_Y0 - 1, 0)))
side = side.union(bwall).union(foot)
sides = mirror_x(side)

# ---------------- front wall ----------------
front = box(-HW, HW, FW_Y, FW_Y + FW_T, -40, -T)
centre_col = box(-SLOT_HW, SLOT_HW, FW_Y, FW_Y + FW_T, -138, -T)
centre_col = centre_col.cut(box(-TUBE_IN_HW, TUBE_IN_HW, FW_Y - 1, FW_Y + FW_T + 1, TUBE_Z0, TUBE_Z1))
centre_col = centre_col.cut(cq.Workplane("XZ").center(0, -118.7).circle(8.6).extrude(-40).translate((0, -10, 0)))
centre_col = centre_col.cut(place(lbox(-HW, HW, -50, 200, BH, BH + 100)))
front = front.union(centre_col)

# ---------------- tilted clamp structure (built in local frame) ----------------
core = lbox(SLOT_HW, CORE_HW, 0, BL, 0, BH)
core = core.cut(lbox(0, HW + 1, GROOVE_U0, BL + 5, GROOVE_V0, GROOVE_V1))
lip = lbox(SLOT_HW, HW, 35, BL, -LIP, 0)
lip = lip.edges("|X").edges("<Y").edges(">Z").fillet(LIP_R)
jaw = lbox(CORE_HW - 0.01, HW, JAW_U0, BL, JAW_V0, JAW_V1)
jfoot = lbox(CORE_HW - 0.01, HW, JAW_U0, BL, FOOTJ_V0, BH)
# bolt hole through the jaw foot (along tilt-normal)
jfoot = jfoot.cut(cq.Workplane("XY").center(JAW_HOLE_X, -JAW_HOLE_U)
                  .circle(2.4).extrude(100).translate((0, 0, -BH - 10)))
jaw = jaw.union(jfoot)
half = core.union(lip).union(jaw)
tilt_l = mirror_x(half)
bridge = lbox(-SLOT_HW - 0.5, SLOT_HW + 0.5, BR_U0, BL, -BR_H, 0)
bridge = bridge.edges("|X").edges("<Y").edges(">Z").fillet(3)
tilt_l = tilt_l.union(bridge)
tilted = place(tilt_l)

body = plate.union(sides).union(front).union(tilted)

# ---------------- rear tube (between box walls) ----------------
tube = box(-WIN_HW - 0.5, WIN_HW + 0.5, TUBE_Y0, TUBE_Y1, WALL_BOT - 0.5, TUBE_TOP)
tube = tube.cut(box(-TUBE_IN_HW, TUBE_IN_HW, TUBE_Y0 - 5, TUBE_Y1 + 5, TUBE_Z0, TUBE_Z1))
body = body.union(tube)

# window shaft through plate
shaft = box(-WIN_HW, WIN_HW, WIN_Y0, WIN_Y1, TUBE_TOP, 1).union(
    box(-NOTCH_HW, NOTCH_HW, WIN_Y0 + 5, NOTCH_Y1, TUBE_TOP, 1))
body = body.cut(shaft)

result = body.val().scale(K)
result = cq.Workplane("XY").add(result)
